import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H = 190.0            # overall height
RB = 50.0            # pipe outer radius
T = 2.5              # pipe wall thickness
OFFSET = 11.7        # lateral offset of the upper pipe (towards -X)
Z_TR_LO = 128.5      # transition start (top of lower straight part)
Z_TR_HI = 152.0      # transition end (bottom of upper straight part)

# threaded ends, modelled as plain V-profile rings (no helix)
BAND_L = 13.4        # axial length of each threaded band
BAND_PITCH = 5.1     # thread pitch
BAND_TEETH = 3       # crests per band
R_TIP = 53.7         # crest radius
R_ROOT = 50.3        # root radius

# top cap
CAP_T = 2.2          # cap thickness
HOLE_D = 15.6        # round hole in the cap (on the upper axis)
SLOT_W = 28.5        # rectangular opening, along X
SLOT_L = 49.2        # rectangular opening, along Y
SLOT_CX = 25.8       # slot centre, X offset from the upper axis
DUCT_WALL = 2.0      # wall of the rectangular duct under the opening
LEAD_D = 1.0         # steep lead-in taper at the top of both openings: depth
LEAD_W = 0.4         # ... and radial width
DUCT_DEPTH = 30.0    # depth of the duct below the top face

VIEW = {"azimuth": 45, "elevation": 26}

XL = OFFSET / 2.0    # lower pipe axis x
XU = -OFFSET / 2.0   # upper pipe axis x


def _seam_back(shape, x):
    """Turn a solid of revolution about its own vertical axis so that its
    seam lies on the -X side (cosmetic only)."""
    return shape.rotate(cq.Vector(x, 0, 0), cq.Vector(x, 0, 1), 180)


def straight(x, r, z0, z1, back=True):
    cyl = cq.Solid.makeCylinder(r, z1 - z0, cq.Vector(x, 0, z0), cq.Vector(0, 0, 1))
    return cq.Workplane("XY").add(_seam_back(cyl, x) if back else cyl)


def _ring(x, z, r, back):
    w = cq.Wire.makeCircle(r, cq.Vector(x, 0, z), cq.Vector(0, 0, 1))
    return _seam_back(w, x) if back else w


def oblique(r, z0, z1, back=True):
    """Ruled (oblique-cylinder) transition between the lower and upper axis."""
    loft = cq.Solid.makeLoft([_ring(XL, z0, r, back), _ring(XU, z1, r, back)], True)
    return cq.Workplane("XY").add(loft)


def band_profile():
    """(r, d) points of a ring band, d measured from the pipe end."""
    d0 = (BAND_L - (BAND_TEETH - 1) * BAND_PITCH) / 2.0   # first crest
    pts = [(RB - T + 0.5, 0.0), (RB, 0.0)]
    for i in range(BAND_TEETH):
        d = d0 + i * BAND_PITCH
        pts.append((R_TIP, d))
        if i < BAND_TEETH - 1:
            pts.append((R_ROOT, d + BAND_PITCH / 2.0))
    pts.append((RB, BAND_L))
    pts.append((RB - T + 0.5, BAND_L))
    return pts, BAND_L


def band(x, at_top):
    pts, length = band_profile()
    if at_top:
        prof = [(r, H - d) for (r, d) in pts]
    else:
        prof = [(r, d) for (r, d) in pts]
    solid = (cq.Workplane("XZ").polyline(prof).close()
             .revolve(360, (0, 0, 0), (0, 1, 0)))
    return solid.rotate((0, 0, 0), (0, 0, 1), 180).translate((x, 0, 0))


# ---------------- outer body ----------------
body = (straight(XL, RB, 0.0, Z_TR_LO)
        .union(oblique(RB, Z_TR_LO, Z_TR_HI))
        .union(straight(XU, RB, Z_TR_HI, H))
        .union(band(XL, False))
        .union(band(XU, True)))

# ---------------- hollow interior (open bottom, closed top cap) ----------------
RI = RB - T
cavity = (straight(XL, RI, -1.0, Z_TR_LO, back=False)
          .union(oblique(RI, Z_TR_LO, Z_TR_HI, back=False))
          .union(straight(XU, RI, Z_TR_HI, H - CAP_T, back=False)))
body = body.cut(cavity)

# ---------------- rectangular duct hanging under the slot ----------------
duct_outer = (cq.Workplane("XY").workplane(offset=H - DUCT_DEPTH)
              .center(XU + SLOT_CX, 0)
              .rect(SLOT_W + 2 * DUCT_WALL, SLOT_L + 2 * DUCT_WALL)
              .extrude(DUCT_DEPTH))
duct_outer = duct_outer.intersect(straight(XU, RI + 0.5, H - DUCT_DEPTH - 1, H))
body = body.union(duct_outer)

# ---------------- openings in the cap ----------------
slot_cut = (cq.Workplane("XY").workplane(offset=H - DUCT_DEPTH - 1)
            .center(XU + SLOT_CX, 0).rect(SLOT_W, SLOT_L)
            .extrude(DUCT_DEPTH + 2))
hole_cut = (cq.Workplane("XY").workplane(offset=H - CAP_T - 1)
            .center(XU, 0).circle(HOLE_D / 2).extrude(CAP_T + 2))
body = body.cut(slot_cut).cut(hole_cut)

# steep lead-in taper on the top edges of both openings
k = 1.0 + 1.0 / LEAD_D            # taper continued 1 mm above the top face
slot_lead = (cq.Workplane("XY").workplane(offset=H - LEAD_D)
             .center(XU + SLOT_CX, 0).rect(SLOT_W, SLOT_L)
             .workplane(offset=LEAD_D + 1.0)
             .rect(SLOT_W + 2 * LEAD_W * k, SLOT_L + 2 * LEAD_W * k)
             .loft(ruled=True))
hole_lead = cq.Workplane("XY").add(
    cq.Solid.makeCone(HOLE_D / 2, HOLE_D / 2 + LEAD_W * k, LEAD_D + 1.0,
                      cq.Vector(XU, 0, H - LEAD_D), cq.Vector(0, 0, 1)))
body = body.cut(slot_lead).cut(hole_lead)

result = body
